"""Oval domed pad / nut.

Oval plan (two small end arcs blended tangentially into two large side arcs),
straight vertical wall, spherical crown on top, and a central hole: a plain
bore from the top that steps down to a tapped hole (thread shown as its minor
diameter) which runs out through the flat underside with an entry countersink.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 60.0            # overall length (X)
W = 29.3            # overall width (Y)
R_END = 10.5        # radius of the two end arcs of the oval plan
H_END = 23.85       # wall height at the two ends of the oval (X = +/-L/2)
H_APEX = 32.5       # height of the spherical crown at the centre (theoretical)
BORE_D = 14.8       # plain bore from the top (= thread major diameter)
TAP_D = 11.7        # tapped hole, thread minor diameter
THREAD_LEN = 17.0   # length of the tapped part, measured from the underside
ENTRY_D = 14.7      # 45 deg entry countersink of the thread at the underside

# ---------------- derived geometry ----------------
a = L / 2.0
b = W / 2.0
# radius of the two long side arcs, tangent to the end arcs
R_SIDE = ((a - R_END) ** 2 + b ** 2 - R_END ** 2) / (2.0 * (b - R_END))
cs = (0.0, -(R_SIDE - b))                 # centre of upper side arc
ce = (a - R_END, 0.0)                     # centre of right end arc
dx, dy = ce[0] - cs[0], ce[1] - cs[1]
dl = math.hypot(dx, dy)
tx = cs[0] + R_SIDE * dx / dl             # tangent point (upper right)
ty = cs[1] + R_SIDE * dy / dl

# spherical crown through (r=a, z=H_END) and (r=0, z=H_APEX)
d = H_APEX - H_END
R_SPH = (a ** 2 + d ** 2) / (2.0 * d)
ZC = H_APEX - R_SPH
H_BLANK = H_APEX + 5.0                    # height of the prism before crowning


# ---------------- oval plan ----------------
def oval_arcs():
    """Exact plan outline: two end arcs (R_END) and two side arcs (R_SIDE),
    all tangent; the left end arc is split so the outline starts at the -X tip."""
    V = cq.Vector
    ex = a - R_END                         # end arc centre offset
    qa = math.atan2(ty, tx - ex)           # angle of the tangent point on the end arc
    pl = (-ex - R_END * math.cos(qa / 2.0), R_END * math.sin(qa / 2.0))
    return [
        cq.Edge.makeThreePointArc(V(-a, 0, 0), V(pl[0], -pl[1], 0), V(-tx, -ty, 0)),
        cq.Edge.makeThreePointArc(V(-tx, -ty, 0), V(0, -b, 0), V(tx, -ty, 0)),
        cq.Edge.makeThreePointArc(V(tx, -ty, 0), V(a, 0, 0), V(tx, ty, 0)),
        cq.Edge.makeThreePointArc(V(tx, ty, 0), V(0, b, 0), V(-tx, ty, 0)),
        cq.Edge.makeThreePointArc(V(-tx, ty, 0), V(pl[0], pl[1], 0), V(-a, 0, 0)),
    ]


def oval_wire():
    """The tangent arcs joined into one exact (rational) B-spline edge, so the
    wall becomes a single smooth face; falls back to the plain arcs if the
    OCC helpers are not reachable."""
    arcs = oval_arcs()
    try:
        from OCP.BRep import BRep_Tool
        from OCP.Geom import Geom_TrimmedCurve
        from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
        from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

        conv = None
        for e in arcs:
            ad = e._geomAdaptor()
            crv = Geom_TrimmedCurve(
                BRep_Tool.Curve_s(e.wrapped, 0.0, 1.0),
                ad.FirstParameter(), ad.LastParameter(),
            )
            if conv is None:
                conv = GeomConvert_CompCurveToBSplineCurve(crv)
            else:
                conv.Add(crv, 1e-6)
        bsp = conv.BSplineCurve()
        bsp.SetPeriodic()
        for i in range(1, bsp.NbKnots() + 1):  # single wall seam at the -X tip
            if abs(bsp.Value(bsp.Knot(i)).X() + a) < 1e-6:
                bsp.SetOrigin(i)
                break
        wire = cq.Wire.assembleEdges([cq.Edge(BRepBuilderAPI_MakeEdge(bsp).Edge())])
        if not wire.IsClosed():
            raise ValueError("open outline")
        return wire
    except Exception:
        return cq.Wire.assembleEdges(arcs)


# ---------------- body: oval prism (ruled between two equal sections) -------
w_bot = oval_wire()
w_top = oval_wire().translate(cq.Vector(0, 0, H_BLANK))
prism = cq.Solid.makeLoft([w_bot, w_top], True)

# spherical crown (sphere turned so that its seam lies far below the part)
sphere = (
    cq.Solid.makeSphere(R_SPH, angleDegrees1=-90, angleDegrees2=90, angleDegrees3=360)
    .rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90)
    .translate(cq.Vector(0, 0, ZC))
)
body = cq.Workplane("XY").add(prism).intersect(cq.Workplane("XY").add(sphere))

# ---------------- central hole ----------------
bore = (                                   # plain bore from the crown down
    cq.Workplane("XY")
    .workplane(offset=THREAD_LEN)
    .circle(BORE_D / 2.0)
    .extrude(H_BLANK - THREAD_LEN)
)
tap = (                                    # tapped part (minor diameter)
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .circle(TAP_D / 2.0)
    .extrude(THREAD_LEN + 2.0)
)
ck = (ENTRY_D - TAP_D) / 2.0               # 45 deg entry countersink
entry = cq.Solid.makeCone(
    ENTRY_D / 2.0 + 1.0, TAP_D / 2.0, ck + 1.0,
    pnt=cq.Vector(0, 0, -1.0), dir=cq.Vector(0, 0, 1),
)
result = body.cut(bore).cut(tap).cut(cq.Workplane("XY").add(entry))

VIEW = {"azimuth": 45, "elevation": 26}
